"""Stackable open sleeve / crate body.

Thick-walled rounded-rectangular tube, open top and bottom:
  * a raised, inset rim on top (step all round the outside),
  * an inner ledge (flange) a little below the rim top with four corner holes,
  * a hand slot through each of the +/-X walls near the top,
  * a stacking recess in the bottom that receives the rim of the unit below.
"""
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
BODY_X = 210.0        # outer size along X
BODY_Y = 186.4        # outer size along Y
BODY_H = 228.2        # height of main body (bottom to outer step)
BODY_R = 10.0         # outer vertical corner radius

RIM_X = 195.6         # outer size of the raised top rim
RIM_Y = 174.0
RIM_R = 8.5           # rim outer corner radius
RIM_H = 9.3           # rim height above the step

WALL = 11.6           # wall thickness (cavity = body - 2*WALL)
IN_R = 7.0            # cavity corner radius

LEDGE_DEPTH = 22.1    # ledge top face below the rim top
LEDGE_T = 4.8         # ledge (inner flange) thickness
OPEN_X = 164.0        # opening through the ledge
OPEN_Y = 140.0
OPEN_R = 16.0         # opening corner radius

HOLE_D = 9.6          # four corner holes through the ledge
HOLE_SX = 170.8       # hole pitch along X
HOLE_SY = 147.4       # hole pitch along Y

SLOT_L = 70.0         # hand slots through the +/-X walls
SLOT_H = 10.4
SLOT_TOP = 32.7       # slot top edge below the outer step
SLOT_R = 0.5          # slot corner radius

REC_X = 197.0         # stacking recess in the bottom face
REC_Y = 175.0
REC_R = 8.0
REC_D = 10.0          # recess depth (>= rim height)

# ---------------- derived ----------------
TOTAL_H = BODY_H + RIM_H
IN_X = BODY_X - 2 * WALL
IN_Y = BODY_Y - 2 * WALL
LEDGE_TOP = TOTAL_H - LEDGE_DEPTH
LEDGE_BOT = LEDGE_TOP - LEDGE_T


def rrect(x, y, r, h, z0=0.0):
    """Rounded rectangle centred on the Z axis, extruded from z0 upward by h."""
    return (cq.Workplane("XY").workplane(offset=z0)
            .sketch().rect(x, y).vertices().fillet(r).finalize()
            .extrude(h))


# main body with the raised rim on top
part = rrect(BODY_X, BODY_Y, BODY_R, BODY_H)
part = part.union(rrect(RIM_X, RIM_Y, RIM_R, RIM_H, BODY_H))

# through cavity (open top and bottom)
part = part.cut(rrect(IN_X, IN_Y, IN_R, TOTAL_H + 2.0, -1.0))

# inner ledge / flange (overlaps the wall slightly so it fuses cleanly)
ledge = rrect(IN_X + 1.0, IN_Y + 1.0, IN_R + 0.5, LEDGE_T, LEDGE_BOT)
ledge = ledge.cut(rrect(OPEN_X, OPEN_Y, OPEN_R, LEDGE_T + 2.0, LEDGE_BOT - 1.0))
part = part.union(ledge)

# four corner holes through the ledge
holes = (cq.Workplane("XY").workplane(offset=LEDGE_BOT - 1.0)
         .rect(HOLE_SX, HOLE_SY, forConstruction=True).vertices()
         .circle(HOLE_D / 2.0).extrude(LEDGE_T + 2.0))
part = part.cut(holes)

# hand slots straight through both X walls
slot_zc = BODY_H - SLOT_TOP - SLOT_H / 2.0
slot = (cq.Workplane("YZ").workplane(offset=-BODY_X)
        .center(0, slot_zc)
        .sketch().rect(SLOT_L, SLOT_H).vertices().fillet(SLOT_R).finalize()
        .extrude(2.0 * BODY_X))
part = part.cut(slot)

# stacking recess in the bottom (takes the rim of the unit below)
part = part.cut(rrect(REC_X, REC_Y, REC_R, REC_D + 1.0, -1.0))

result = part

VIEW = {"azimuth": 45, "elevation": 26}
